import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------
# Driving dimensions (mm).  X = across, Y = length, Z = height
# ---------------------------------------------------------------
L = 100.0          # overall length (Y)
H = 45.0           # overall height (Z)

# main side plate (at +X)
PL_IN = 69.0       # inner face of plate
PL_UP = 75.8       # outer face of upper band
PL_LO = 78.4       # outer face of lower region
Z_BAND = 29.3      # height where upper band starts
END_CH = 1.5       # chamfer on the -Y vertical edge of lower region

BOT_CH = 0.8        # small chamfer on all bottom edges

# hook lip at the -Y end
HOOK_X = 60.1
HOOK_T = 7.0
HOOK_R = 3.3

# block at the +Y end
BLK_Y0 = 54.6
BLK_LO_X = 43.1     # lower block inner face
BLK_UP_X = 54.8     # upper block inner face
Z_FLOOR = 21.0      # slot floor height
WALL_X = 45.6       # back wall inner face
WALL_Y = 93.7       # back wall front face
CH_X, CH_Y = 8.8, 10.5   # chamfer on lower block (-X,-Y) vertical edge
CH_R = 3.0
SLOT_FIL = 3.5

# upper body / column at -X
COL_W = 12.0
COL_LEDGE = 14.9
COL_Y0 = 74.1
UB_Y0 = 77.0
Z_UB = 19.5
RIB_X0, RIB_X1 = 26.0, 32.3
SLANT = ((20.6, L), (0.0, 95.2))   # slanted back edge of the column


def slant_y(x):
    (x0, y0), (x1, y1) = SLANT
    return y1 + (x - x1) * (y0 - y1) / (x0 - x1)


# holes
Y_VH = 87.0
VH_X = (7.45, 29.2, 59.2)
D_SMALL = 5.8
D_CB_BOT = 10.0
CB_BOT_DEPTH = 3.0

Z_UH = 37.2
Y_UH1, Y_UH2, Y_UH3 = 22.1, 56.5, 91.1
D_UH = 5.5
D_UH_BIG = 8.4
UH_BIG_DEPTH = 16.0
HEX_AF = 9.6
HEX_DEPTH = 4.0

CB_Y = (13.3, 47.8)
CB_Z = 20.0
CB_D_TOP = 14.6
CB_D = 11.7
CB_DEPTH = 2.6
CB_CONE_DEPTH = 1.8       # shallow conical floor of the counterbore

WIN_Y0, WIN_Y1 = 62.9, 74.2
WIN_Z0, WIN_Z1 = 4.0, 25.5
KEY_Y1 = 82.1                 # end of key slot
KEY_Z0, KEY_Z1 = 11.4, 18.5
KEY_R_END = 1.8
KEY_NECK_L, KEY_NECK_R = 4.2, 5.4   # length and radius of the flared neck
KEY_X0 = 55.0                 # key slot runs from here to the outer face
USLOT_ZC, USLOT_DEPTH = 30.6, 1.5
UHOLE_Y, UHOLE_Z, UHOLE_D, UHOLE_DEPTH = 70.0, 31.0, 6.5, 8.0

# angled boss
BOSS_PHI = 26.0          # deg, normal of the boss end face, from +X toward -Y
BOSS_Y_EDGE = 21.4       # where boss face B meets the plate
BOSS_XMAX = 85.4
BOSS_YMAX = 46.2
BOSS_ZTOP = 18.5
BOSS_HOLE_Y, BOSS_HOLE_Z = 29.7, 8.9
BOSS_CS_D = 11.0          # countersink diameter on the end face
BOSS_CS_HALF_ANGLE = 45.0
BOSS_HOLE_D = 5.8
BOSS_HOLE_X0 = 79.3        # flat bottom of the blind hole
BOSS_BOT_CH = 1.2


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def near(x, y, z, tol=0.6):
    return cq.selectors.BoxSelector((x - tol, y - tol, z - tol), (x + tol, y + tol, z + tol))


def vsel(x, y, z0, z1, tol=0.5):
    """Select (vertical) edges passing near (x, y) between z0 and z1."""
    return cq.selectors.BoxSelector((x - tol, y - tol, z0), (x + tol, y + tol, z1))


def prism(pts, z0, z1):
    return cq.Workplane("XY").polyline(pts).close().extrude(z1 - z0).translate((0, 0, z0))


YZ = cq.Plane(origin=(0, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))


def xcyl(y, z, d, x0, x1):
    return cq.Workplane(YZ).center(y, z).circle(d / 2).extrude(x1 - x0).translate((x0, 0, 0))


# ---------------------------------------------------------------
# plate + hook
# ---------------------------------------------------------------
plate = box(PL_IN, PL_LO, 0, L, 0, Z_BAND)
plate = plate.edges(near(PL_LO, 0, Z_BAND / 2)).chamfer(END_CH)
plate = plate.union(box(PL_IN, PL_UP, 0, L, Z_BAND, H))

hook = box(HOOK_X, PL_IN + 0.01, 0, HOOK_T, 0, H)
hook = hook.edges(near(HOOK_X, 0, H / 2)).fillet(HOOK_R)
hook = hook.edges(near(HOOK_X, HOOK_T, H / 2)).fillet(HOOK_R)

# ---------------------------------------------------------------
# block at the +Y end (lower part, upper part, back wall)
# ---------------------------------------------------------------
blk_lo = prism([
    (BLK_LO_X, L), (BLK_LO_X, BLK_Y0 + CH_Y), (BLK_LO_X + CH_X, BLK_Y0),
    (PL_IN + 0.01, BLK_Y0), (PL_IN + 0.01, L)], 0, Z_FLOOR)
blk_up = box(BLK_UP_X, PL_IN + 0.01, BLK_Y0, L, 0, H)
wall = box(WALL_X, BLK_UP_X + 0.01, WALL_Y, L, 0, H)
blk_lo = blk_lo.edges(vsel(BLK_LO_X, BLK_Y0 + CH_Y, -1, H, 0.3)).fillet(CH_R)
block = blk_lo.union(blk_up).union(wall)
block = block.edges(near(WALL_X, L, (Z_FLOOR + H) / 2, 1.0)).fillet(3.0)
sel = (cq.selectors.BoxSelector((BLK_UP_X - 0.5, BLK_Y0 + 1, Z_FLOOR - 0.5), (BLK_UP_X + 0.5, WALL_Y + 0.5, Z_FLOOR + 0.5))
       + cq.selectors.BoxSelector((BLK_UP_X - 0.5, WALL_Y - 0.5, Z_FLOOR + 1), (BLK_UP_X + 0.5, WALL_Y + 0.5, H - 1))
       + cq.selectors.BoxSelector((WALL_X + 0.5, WALL_Y - 0.5, Z_FLOOR - 0.5), (BLK_UP_X - 0.5, WALL_Y + 0.5, Z_FLOOR + 0.5)))
block = block.edges(sel).fillet(SLOT_FIL)

# ---------------------------------------------------------------
# upper body: column + lower bridge + rib
# ---------------------------------------------------------------
bridge = prism([(COL_LEDGE - 0.01, UB_Y0), (BLK_LO_X + 0.01, UB_Y0), (BLK_LO_X + 0.01, L),
                SLANT[0], (COL_LEDGE - 0.01, slant_y(COL_LEDGE - 0.01))], 0, Z_UB)
bridge = bridge.edges(cq.selectors.BoxSelector((COL_LEDGE + 1, UB_Y0 - 0.5, Z_UB - 0.5),
                                               (BLK_LO_X - 1, UB_Y0 + 0.5, Z_UB + 0.5))).fillet(3.0)

column = prism([(0, COL_Y0), (COL_LEDGE, COL_Y0), (COL_LEDGE, slant_y(COL_LEDGE)), SLANT[1]], 0, Z_FLOOR)
column = column.union(prism([(0, COL_Y0), (COL_W, COL_Y0), (COL_W, slant_y(COL_W)), SLANT[1]], 0, H))

column = column.edges(vsel(0, COL_Y0, 0, H)).fillet(4.5)
column = column.edges(vsel(0, SLANT[1][1], 0, H)).fillet(7.0)
column = column.edges(vsel(COL_W, COL_Y0, Z_FLOOR + 1, H)).fillet(2.0)
column = column.edges(vsel(COL_W, slant_y(COL_W), Z_FLOOR + 1, H)).fillet(1.0)

rib = box(RIB_X0, RIB_X1, COL_Y0, L, 0, Z_FLOOR)

body = plate.union(hook).union(block).union(bridge).union(column).union(rib)
body = body.edges(cq.selectors.BoxSelector((-5, -5, -0.05), (L, L + 5, 0.05))).chamfer(BOT_CH)

# ---------------------------------------------------------------
# angled boss on the outer face (half-space intersection)
# ---------------------------------------------------------------
phi = math.radians(BOSS_PHI)
nB = cq.Vector(math.cos(phi), -math.sin(phi), 0)


def halfspace(origin, normal, size=300.0):
    """Solid occupying the side of the plane opposite to the normal."""
    n = cq.Vector(normal).normalized()
    xd = n.cross(cq.Vector(0, 0, 1)) if abs(n.z) < 0.99 else cq.Vector(1, 0, 0)
    pl = cq.Plane(origin=cq.Vector(origin), xDir=xd, normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(-size)


boss = box(PL_LO - 2.0, BOSS_XMAX, BOSS_Y_EDGE - 2.0, BOSS_YMAX + 2.0, 0.0, BOSS_ZTOP + 2)
# end face (B), vertical, carries the countersink
boss = boss.intersect(halfspace((PL_LO, BOSS_Y_EDGE, 0), nB))
# facets around the end face, each given by a point on the plate face and an outward normal
for org, nrm in (
        ((PL_LO, BOSS_Y_EDGE, 10.3), (-0.267, -0.905, 0.331)),   # small upper-left facet
        ((PL_LO, 0.0, BOSS_ZTOP), (0.667, 0.0, 0.745)),           # top facet
        ((PL_LO, 35.0, BOSS_ZTOP), (0.689, 0.496, 0.529)),        # upper-right facet
        ((PL_LO, 44.6, 9.3), (0.813, 0.549, 0.193)),              # right facet
        ((PL_LO, BOSS_YMAX, 0.0), (0.871, 0.460, -0.175)),        # lower-right facet
):
    boss = boss.intersect(halfspace(org, nrm))
p_bot = cq.Vector(PL_LO, BOSS_Y_EDGE, 0) - nB * BOSS_BOT_CH
boss = boss.intersect(halfspace(p_bot.toTuple(), (nB.x * 0.707, nB.y * 0.707, -0.707)))  # bottom chamfer
body = body.union(boss)

# ---------------------------------------------------------------
# holes and cut-outs
# ---------------------------------------------------------------
cuts = []
# vertical holes with counterbore on the underside
for x in VH_X:
    cuts.append(cq.Workplane("XY").center(x, Y_VH).circle(D_SMALL / 2).extrude(H + 2).translate((0, 0, -1)))
    cuts.append(cq.Workplane("XY").center(x, Y_VH).circle(D_CB_BOT / 2).extrude(CB_BOT_DEPTH + 1).translate((0, 0, -1)))

# holes in the upper band (along X)
cuts.append(xcyl(Y_UH1, Z_UH, D_UH, 55.0, 90.0))
cuts.append(xcyl(Y_UH2, Z_UH, D_UH, PL_IN, 90.0))
cuts.append(xcyl(Y_UH3, Z_UH, D_UH_BIG, PL_UP - UH_BIG_DEPTH, 90.0))
# hex nut trap on the inner face
for y in (Y_UH1, Y_UH2):
    cuts.append(cq.Workplane(YZ).center(y, Z_UH).polygon(6, HEX_AF / math.cos(math.pi / 6))
                .extrude(HEX_DEPTH + 1).translate((PL_IN - 1, 0, 0)))

# counterbored holes in the lower region
for y in CB_Y:
    cuts.append(xcyl(y, CB_Z, D_SMALL, 55.0, 90.0))
    cone = cq.Solid.makeCone(CB_D / 2, CB_D_TOP / 2 + 0.3, CB_DEPTH + 0.3,
                             pnt=cq.Vector(PL_LO - CB_DEPTH, y, CB_Z), dir=cq.Vector(1, 0, 0))
    cuts.append(cq.Workplane().add(cone))
    cone2 = cq.Solid.makeCone(D_SMALL / 2, CB_D / 2, CB_CONE_DEPTH + 0.01,
                              pnt=cq.Vector(PL_LO - CB_DEPTH - CB_CONE_DEPTH, y, CB_Z), dir=cq.Vector(1, 0, 0))
    cuts.append(cq.Workplane().add(cone2))

# window + key slot through the part (profile in the YZ plane)
kz0, kz1, r1 = KEY_Z0, KEY_Z1, KEY_R_END
c45 = math.cos(math.pi / 4)
nl, nr = KEY_NECK_L, KEY_NECK_R
nd = nr - math.sqrt(nr ** 2 - nl ** 2)                 # drop of the neck arc at the window edge
am = math.atan2(-(nr - nd), -nl) / 2 - math.pi / 4      # mid angle of the neck arc
mid_dy, mid_dz = nl + nr * math.cos(am), nr + nr * math.sin(am)
win = (
    cq.Workplane(YZ)
    .moveTo(WIN_Y0, WIN_Z0)
    .lineTo(WIN_Y1, WIN_Z0)
    .lineTo(WIN_Y1, kz0 - nd)
    .threePointArc((WIN_Y1 + mid_dy, kz0 - mid_dz), (WIN_Y1 + nl, kz0))
    .lineTo(KEY_Y1 - r1, kz0)
    .threePointArc((KEY_Y1 - r1 + r1 * c45, kz0 + r1 - r1 * c45), (KEY_Y1, kz0 + r1))
    .lineTo(KEY_Y1, kz1 - r1)
    .threePointArc((KEY_Y1 - r1 + r1 * c45, kz1 - r1 + r1 * c45), (KEY_Y1 - r1, kz1))
    .lineTo(WIN_Y1 + nl, kz1)
    .threePointArc((WIN_Y1 + mid_dy, kz1 + mid_dz), (WIN_Y1, kz1 + nd))
    .lineTo(WIN_Y1, WIN_Z1)
    .lineTo(WIN_Y0, WIN_Z1)
    .close()
    .extrude(PL_LO + 2.0 - KEY_X0)
    .translate((KEY_X0, 0, 0))
)
cuts.append(win)
cuts.append(box(BLK_LO_X - 0.01, PL_LO + 2.0, WIN_Y0, WIN_Y1, WIN_Z0, WIN_Z1))
# rounded-top pocket on the inner side of the upper block (inside the slot)
uw = WIN_Y1 - WIN_Y0
upocket = (
    cq.Workplane(YZ).center((WIN_Y0 + WIN_Y1) / 2, 0)
    .moveTo(-uw / 2, WIN_Z0).lineTo(uw / 2, WIN_Z0).lineTo(uw / 2, USLOT_ZC)
    .threePointArc((0, USLOT_ZC + uw / 2), (-uw / 2, USLOT_ZC)).close()
    .extrude(USLOT_DEPTH + SLOT_FIL + 0.5)
    .translate((BLK_UP_X - SLOT_FIL - 0.5, 0, 0))
)
cuts.append(upocket)
cuts.append(xcyl(UHOLE_Y, UHOLE_Z, UHOLE_D, BLK_UP_X, BLK_UP_X + USLOT_DEPTH + UHOLE_DEPTH))

# boss: short blind hole along X, countersink normal to the end face
cuts.append(xcyl(BOSS_HOLE_Y, BOSS_HOLE_Z, BOSS_HOLE_D, BOSS_HOLE_X0, 95.0))
p_cs = cq.Vector(PL_LO + (BOSS_HOLE_Y - BOSS_Y_EDGE) * math.tan(phi), BOSS_HOLE_Y, BOSS_HOLE_Z)
cs_depth = (BOSS_CS_D - BOSS_HOLE_D) / 2 / math.tan(math.radians(BOSS_CS_HALF_ANGLE))
cuts.append(cq.Workplane().add(cq.Solid.makeCone(
    BOSS_HOLE_D / 2, BOSS_CS_D / 2 + 0.5 * math.tan(math.radians(BOSS_CS_HALF_ANGLE)), cs_depth + 0.5,
    pnt=p_cs - nB * cs_depth, dir=nB)))

for c in cuts:
    body = body.cut(c)

result = body
